import math
import cadquery as cq

# ------------------------------------------------------------------
# Driving dimensions (mm)
# ------------------------------------------------------------------
# Base plate (main fixture)
BP_L, BP_W, BP_T, BP_R = 166.3, 84.4, 6.0, 6.0

# Frame (lower cup + top ring + two struts) on the base plate
FR_X, FR_Y = -47.9, 0.0
CYL_R = 26.8          # outer radius of lower cylinder and top ring
CYL_TOP = 38.6        # top of lower cylinder (from z=0)
CB_R, CB_D = 24.8, 5.0   # counterbore in lower cylinder
BORE_R, BORE_BOT = 12.3, 2.0
RING_IN = 24.2
RING_Z0, RING_Z1 = 95.4, 105.1
RING_GAP = 1.0
STRUT_W = 10.6
STRUT_IN, STRUT_OUT, STRUT_BASE = 24.0, 33.0, 38.8
STRUT_FLARE_Z = 49.0
STRUT_TOP_R = 4.5

# Posts with brackets
POST_W, POST_L = 9.0, 19.4
POST_TOP = 99.3
POST_HOLE_D, POST_HOLE_DEPTH = 7.0, 15.0
POST_XS = (0.0, 72.2)
POST_YS = (23.8, -23.8)
BRK_TOP, BRK_T = 61.25, 6.75
BRK_REACH = 19.5          # distance from post centre to bracket tip
BRK_FIL = 4.5             # concave fillet under the bracket
BRK_CORNER_R = 4.6
BRK_NOSE_R = 3.0

# Slabs (D-shaped: outer vertical edges rounded)
SLAB_T, SLAB_L, SLAB_TOP = 7.2, 23.5, 98.5
SLAB_EDGE_R, SLAB_TOP_R = 2.5, 3.0
SLAB_XS = (10.4, 30.8)

# U plates (loose parts in front)
UP_T = 5.1
UP_Y0, UP_Y1 = -128.65, -61.75
UP_SLOT_Y0, UP_SLOT_Y1 = -109.55, -80.55
UP_IN_R = 4.0

# Pin plate
PP_X0, PP_X1 = 2.1, 83.6
PP_SLOT_X0 = 20.6
PP_R = 5.0
PP_HOLE_D = 6.5
PP_HOLES = [(6.4, -71.55), (77.6, -71.55), (6.4, -118.55), (77.6, -118.55)]
PIN_D, PIN_TOP = 9.8, 38.5
PINS = [(43.6, -71.55), (43.6, -118.55), (12.9, -94.55)]

# Notched plate
NP_X0, NP_X1 = -100.8, -26.2
NP_SLOT_X1 = -45.0
NP_ARC_SAG = 3.0
NOTCH_X, NOTCH_R, NOTCH_LEN = -30.8, 5.0, 19.2

# Arm (cup + bent strap + top bar)
CUP_X, CUP_Y, CUP_R, CUP_H = -130.0, -38.55, 22.75, 12.0
CUP_WALL, CUP_FLOOR = 2.0, 5.5
STRAP_W, STRAP_T = 12.4, 6.8
STRAP_FRONT_Y = 26.3
STRAP_BEND_Z = 38.0
STRAP_DIAG_END_Y = -6.0
STRAP_BEND_RI = 2.5       # inner bend radius
STRAP_FIL = 4.0           # blend radius strap/bar and strap/cup
BAR_L, BAR_W, BAR_T, BAR_R = 48.0, 12.0, 5.3, 2.0
BAR_Y0 = 24.0
BAR_Z0 = 106.0


# ------------------------------------------------------------------
# helpers
# ------------------------------------------------------------------
SEAM_OUT, SEAM_IN = 135.0, -45.0   # keep cylinder seams on hidden sides


def zcyl(r, h, x, y, z0, seam=SEAM_OUT):
    """Vertical cylinder with its seam rotated to a hidden side."""
    c = cq.Solid.makeCylinder(r, h, cq.Vector(0, 0, z0), cq.Vector(0, 0, 1))
    c = c.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), seam)
    return cq.Workplane("XY").add(c.translate(cq.Vector(x, y, 0)))


def rounded_profile(wp, pts, radii):
    """Closed 2D profile through pts with tangent arcs of given radii."""
    n = len(pts)
    segs = []
    for i in range(n):
        p = pts[i]
        r = radii[i]
        if r <= 0:
            segs.append((p, None, p))
            continue
        a, b = pts[i - 1], pts[(i + 1) % n]
        u1 = (a[0] - p[0], a[1] - p[1])
        u2 = (b[0] - p[0], b[1] - p[1])
        l1, l2 = math.hypot(*u1), math.hypot(*u2)
        u1 = (u1[0] / l1, u1[1] / l1)
        u2 = (u2[0] / l2, u2[1] / l2)
        th = math.acos(max(-1.0, min(1.0, u1[0] * u2[0] + u1[1] * u2[1])))
        d = r / math.tan(th / 2)
        t1 = (p[0] + u1[0] * d, p[1] + u1[1] * d)
        t2 = (p[0] + u2[0] * d, p[1] + u2[1] * d)
        bx, by = u1[0] + u2[0], u1[1] + u2[1]
        bl = math.hypot(bx, by)
        bx, by = bx / bl, by / bl
        h = r / math.sin(th / 2)
        c = (p[0] + bx * h, p[1] + by * h)
        m = (c[0] - bx * r, c[1] - by * r)
        segs.append((t1, m, t2))
    w = wp.moveTo(*segs[0][2])
    for i in range(1, n + 1):
        t1, m, t2 = segs[i % n]
        w = w.lineTo(*t1)
        if m is not None:
            w = w.threePointArc(m, t2)
    return w.close()


def fillet_profile(wp, x0, z0, r, sx=1, sz=-1):
    """Square r x r at (x0, z0) minus quarter circle -> concave fillet."""
    return (wp.moveTo(x0, z0)
            .lineTo(x0 + sx * r, z0)
            .threePointArc((x0 + sx * r * (1 - math.sqrt(0.5)),
                            z0 + sz * r * (1 - math.sqrt(0.5))),
                           (x0, z0 + sz * r))
            .close())


# ------------------------------------------------------------------
# Base plate with frame, posts and slabs
# ------------------------------------------------------------------
base = (cq.Workplane("XY").rect(BP_L, BP_W).extrude(BP_T)
        .edges("|Z").fillet(BP_R))

# lower cylinder
cyl = zcyl(CYL_R, CYL_TOP - BP_T + 0.5, FR_X, FR_Y, BP_T - 0.5)
# top ring
ring = zcyl(CYL_R, RING_Z1 - RING_Z0, FR_X, FR_Y, RING_Z0).cut(
    zcyl(RING_IN, RING_Z1 - RING_Z0 + 2, FR_X, FR_Y, RING_Z0 - 1, SEAM_IN))


def strut(sign):
    # side profile in the YZ plane (outer face flares towards the base)
    pts = [
        (STRUT_IN, BP_T - 0.5),
        (STRUT_BASE, BP_T - 0.5),
        (STRUT_BASE, BP_T),
        (STRUT_OUT, STRUT_FLARE_Z),
        (STRUT_OUT, RING_Z1),
        (STRUT_IN, RING_Z1),
    ]
    prof = (cq.Workplane("YZ", origin=(FR_X - STRUT_W / 2, 0, 0))
            .polyline(pts).close().extrude(STRUT_W))
    # round the outer top edge
    prof = prof.edges("|X").edges(">Z").edges(">Y").fillet(STRUT_TOP_R)
    if sign < 0:
        prof = prof.mirror("XZ", basePointVector=(0, FR_Y, 0))
    return prof


frame = cyl.union(ring).union(strut(1)).union(strut(-1))
# counterbore and bore in the lower cylinder
frame = frame.cut(zcyl(CB_R, CB_D + 1, FR_X, FR_Y, CYL_TOP - CB_D, SEAM_IN))
frame = frame.cut(zcyl(BORE_R, CYL_TOP, FR_X, FR_Y, BORE_BOT, SEAM_IN))
# splits in the ring at +/-X
for sx in (1, -1):
    frame = frame.cut(cq.Workplane("XY").workplane(offset=RING_Z0 - 0.1)
                      .center(FR_X + sx * (CYL_R - 1.5), FR_Y)
                      .rect(5, RING_GAP).extrude(RING_Z1 - RING_Z0 + 1))

main = base.union(frame)


def post_with_bracket():
    """Post at origin with its bracket pointing towards +X."""
    hw = POST_W / 2
    half_straight = POST_L / 2 - hw
    p = (cq.Workplane("XY").workplane(offset=BP_T - 0.5)
         .slot2D(POST_L, POST_W, 90).extrude(POST_TOP - BP_T + 0.5))
    p = p.cut(zcyl(POST_HOLE_D / 2, POST_HOLE_DEPTH + 1, 0, 0,
                   POST_TOP - POST_HOLE_DEPTH, SEAM_IN))

    zb = BRK_TOP - BRK_T
    # side profile (rounded lower tip edge) intersected with the plan
    # outline (rounded tip corners)
    prof = rounded_profile(
        cq.Workplane("XZ", origin=(0, POST_L / 2, 0)),
        [(0, zb), (BRK_REACH, zb), (BRK_REACH, BRK_TOP), (0, BRK_TOP)],
        [0, BRK_NOSE_R, 0, 0]).extrude(POST_L)
    plan = (cq.Workplane("XY").workplane(offset=zb - 1)
            .center(BRK_REACH / 2, 0).rect(BRK_REACH, POST_L)
            .extrude(BRK_T + 2).edges("|Z").edges(">X").fillet(BRK_CORNER_R))
    brk = prof.intersect(plan)

    # concave fillet under the bracket: straight part + two quarter revolves
    r = BRK_FIL
    fil = fillet_profile(cq.Workplane("XZ", origin=(0, half_straight, 0)),
                         hw, zb, r).extrude(2 * half_straight)
    for s in (1, -1):
        q = fillet_profile(cq.Workplane("XZ", origin=(0, s * half_straight, 0)),
                           hw, zb, r)
        q = q.revolve(90, (0, zb, 0), (0, zb + 1, 0))
        if s < 0:
            q = q.mirror("XZ", basePointVector=(0, -half_straight, 0))
        fil = fil.union(q)
    clip = (cq.Workplane("XY").workplane(offset=zb - r - 1)
            .center(BRK_REACH / 2, 0)
            .rect(BRK_REACH, POST_L).extrude(r + 1))
    fil = fil.intersect(clip)
    return p.union(brk).union(fil)


pwb = post_with_bracket()
for px, dirn in ((POST_XS[0], 1), (POST_XS[1], -1)):
    for py in POST_YS:
        inst = pwb if dirn > 0 else pwb.mirror("YZ")
        main = main.union(inst.translate((px, py, 0)))


def slab(outer_sign):
    s = (cq.Workplane("XY").workplane(offset=BP_T - 0.5)
         .rect(SLAB_T, SLAB_L).extrude(SLAB_TOP - BP_T + 0.5))
    sel_out = ">X" if outer_sign > 0 else "<X"
    s = s.edges("|Z").edges(sel_out).fillet(SLAB_EDGE_R)
    inner_x = -outer_sign * SLAB_T / 2
    top_edges = [e for e in s.faces(">Z").edges().vals()
                 if abs(e.Center().x - inner_x) > 0.3]
    s = s.newObject(top_edges).fillet(SLAB_TOP_R)
    return s


for sx, osign in ((SLAB_XS[0], -1), (SLAB_XS[1], 1)):
    main = main.union(slab(osign).translate((sx, 0, 0)))

# ------------------------------------------------------------------
# Pin plate (U open towards +X) with three pins
# ------------------------------------------------------------------
up_cy = (UP_Y0 + UP_Y1) / 2
up_w = UP_Y1 - UP_Y0
slot_w = UP_SLOT_Y1 - UP_SLOT_Y0
slot_cy = (UP_SLOT_Y0 + UP_SLOT_Y1) / 2

pp = (cq.Workplane("XY").center((PP_X0 + PP_X1) / 2, up_cy)
      .rect(PP_X1 - PP_X0, up_w).extrude(UP_T).edges("|Z").fillet(PP_R))
pp_open = (cq.Workplane("XY").workplane(offset=-1)
           .center((PP_SLOT_X0 + PP_X1 + 10) / 2, slot_cy)
           .rect(PP_X1 + 10 - PP_SLOT_X0, slot_w).extrude(UP_T + 2)
           .edges("|Z").edges("<X").fillet(UP_IN_R))
pp = pp.cut(pp_open)
for hx, hy in PP_HOLES:
    pp = pp.cut(zcyl(PP_HOLE_D / 2, UP_T + 2, hx, hy, -1, SEAM_IN))
for px_, py_ in PINS:
    pp = pp.union(zcyl(PIN_D / 2, PIN_TOP - UP_T + 0.5, px_, py_, UP_T - 0.5))

# ------------------------------------------------------------------
# Notched plate (U open towards -X)
# ------------------------------------------------------------------
np_ = (cq.Workplane("XY").center((NP_X0 + NP_X1) / 2, up_cy)
       .rect(NP_X1 - NP_X0, up_w).extrude(UP_T))
np_open = (cq.Workplane("XY").workplane(offset=-1)
           .center((NP_X0 - 10 + NP_SLOT_X1) / 2, slot_cy)
           .rect(NP_SLOT_X1 - NP_X0 + 10, slot_w).extrude(UP_T + 2)
           .edges("|Z").edges(">X").fillet(UP_IN_R))
np_ = np_.cut(np_open)
# concave ends of the two arms
arm_w = UP_Y1 - UP_SLOT_Y1
arc_r = (arm_w ** 2 / 4 + NP_ARC_SAG ** 2) / (2 * NP_ARC_SAG)
for acy in ((UP_Y1 + UP_SLOT_Y1) / 2, (UP_Y0 + UP_SLOT_Y0) / 2):
    np_ = np_.cut(zcyl(arc_r, UP_T + 2, NP_X0 + NP_ARC_SAG - arc_r, acy, -1,
                       180.0))
# obround notches at the two right-hand corners
for s in (1, -1):
    ny = up_cy + s * (up_w / 2 - NOTCH_LEN / 2 + 0.1)
    np_ = np_.cut(cq.Workplane("XY").workplane(offset=-1).center(NOTCH_X, ny)
                  .slot2D(NOTCH_LEN, 2 * NOTCH_R, 90).extrude(UP_T + 2))
    top_c = ny + s * (NOTCH_LEN / 2 - NOTCH_R)
    np_ = np_.cut(cq.Workplane("XY").workplane(offset=-1)
                  .center(NOTCH_X + 5, top_c + s * 5).rect(10, 10)
                  .extrude(UP_T + 2))

# ------------------------------------------------------------------
# Arm: cup, bent strap and top bar
# ------------------------------------------------------------------
cup = zcyl(CUP_R, CUP_H, CUP_X, CUP_Y, 0)

# strap side profile in YZ
dy = STRAP_DIAG_END_Y - STRAP_FRONT_Y
dz = CUP_H - STRAP_BEND_Z
L = math.hypot(dy, dz)
ux, uz = dy / L, dz / L
nx, nz = -uz, ux
if nz > 0:
    nx, nz = -nx, -nz
ix0, iz0 = STRAP_FRONT_Y + nx * STRAP_T, STRAP_BEND_Z + nz * STRAP_T
back_y = STRAP_FRONT_Y + STRAP_T
t1 = (back_y - ix0) / ux
b1 = (back_y, iz0 + uz * t1)
bot_z = CUP_H - STRAP_T
t2 = (bot_z - iz0) / uz
b2 = (ix0 + ux * t2, bot_z)
rim_y = CUP_Y + CUP_R - 1.2
ri, ro = STRAP_BEND_RI, STRAP_BEND_RI + STRAP_T
strap_pts = [
    (STRAP_FRONT_Y, BAR_Z0 + 0.5),
    (STRAP_FRONT_Y, STRAP_BEND_Z),
    (STRAP_DIAG_END_Y, CUP_H),
    (rim_y, CUP_H),
    (rim_y, bot_z),
    b2,
    b1,
    (back_y, BAR_Z0 + 0.5),
]
strap_r = [0, ri, ro, 0, 0, ri, ro, 0]
strap = rounded_profile(cq.Workplane("YZ", origin=(CUP_X - STRAP_W / 2, 0, 0)),
                        strap_pts, strap_r).extrude(STRAP_W)
bar = (cq.Workplane("XY").workplane(offset=BAR_Z0)
       .center(CUP_X, BAR_Y0 + BAR_W / 2).rect(BAR_L, BAR_W).extrude(BAR_T)
       .edges("|Z").fillet(BAR_R))
arm = cup.union(strap).union(bar)

# blends strap <-> bar (in XZ) on both sides of the strap
for s in (1, -1):
    xe = CUP_X + s * STRAP_W / 2
    blk = fillet_profile(cq.Workplane("XZ", origin=(0, back_y, 0)),
                         xe, BAR_Z0, STRAP_FIL, sx=s, sz=-1).extrude(STRAP_T)
    arm = arm.union(blk)

# blends strap <-> cup (in plan) on both sides of the strap
rf = STRAP_FIL
for s in (1, -1):
    xe = CUP_X + s * STRAP_W / 2
    cx = xe + s * rf
    cy = CUP_Y + math.sqrt((CUP_R + rf) ** 2 - (STRAP_W / 2 + rf) ** 2)
    blk = (cq.Workplane("XY").workplane(offset=bot_z)
           .center(xe + s * rf / 2, cy - 2.0).rect(rf, 4.0).extrude(STRAP_T))
    blk = blk.cut(zcyl(rf, STRAP_T + 2, cx, cy, bot_z - 1, 90.0))
    arm = arm.union(blk)

arm = arm.cut(zcyl(CUP_R - CUP_WALL, CUP_H, CUP_X, CUP_Y, CUP_FLOOR, SEAM_IN))

# imprint the cylinder and bore outlines on the underside of the base plate
_main = main.val()
_split = _main.split(
    cq.Face.makeFromWires(cq.Wire.makeCircle(CYL_R, cq.Vector(FR_X, FR_Y, 0),
                                             cq.Vector(0, 0, 1))),
    cq.Face.makeFromWires(cq.Wire.makeCircle(BORE_R, cq.Vector(FR_X, FR_Y, 0),
                                             cq.Vector(0, 0, 1))))
if len(_split.Solids()) == 1:
    main = cq.Workplane("XY").add(_split.Solids()[0])

result = cq.Workplane("XY").add(cq.Compound.makeCompound(
    [main.val(), pp.val(), np_.val(), arm.val()]))
